import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
W = 100.0          # overall width (X)
L = 92.5           # overall length (Y)
H = 15.0           # block height
GAP = 7.5          # slot between the two halves
R_V = 3.5          # vertical corner radius (plan view)
R_TOP = 3.7        # top edge fillet
C_BOT = 1.5        # bottom edge chamfer
R_BACK_IN = 1.0    # small radius at the rear inner corner of the floor
Z_PART = 5.5       # parting line height
STEP = 0.25        # inset of the upper shell at the parting line

CH_HALF = 27.6     # half width of the U-channel at the back
U_R = 28.0         # radius of the U end of the channel
U_Y = 19.2         # centre of the U end
Z_FLOOR = 4.3      # channel floor height

LEDGE_IN = 22.6    # inner face of the side ledges
LEDGE_Z = 11.4     # top of the ledges
LEDGE_END_R = 6.6  # rounded end of the ledge around the screw boss

DISK_Y = 18.3      # centre of the turntable disk
DISK_R = 20.3      # outer ring radius
DISK_R2 = 18.7     # raised inner body radius
DISK_Z0 = 0.3      # disk underside (slightly recessed)
Z_RING = 8.1       # ring top / cross pocket floor
Z_PAD = 10.8       # top of the quadrant pads
ARM_Y_W = 11.2     # width of cross arm along Y
ARM_Y_L = 16.6     # reach of the Y arm from the centre
ARM_X_W = 15.8     # width of cross arm along X
ARM_R = 2.5        # corner radius of the Y arm ends
HOLE_C = 12.8      # central through hole
HOLE_S = 3.8       # small holes
HOLE_S_CB = 6.8    # small hole counterbore (underside)
HOLE_S_R = 12.0    # radius of small hole circle
DISK_REC_R = 16.0  # shallow recess on the disk underside

FOOT_X = 29.5      # obround foot centre x
FOOT_W = 13.7      # obround foot width
HOLE_Y1 = 23.4     # rear screw hole y
HOLE_P = 14.6      # screw hole pitch
FOOT_H = 3.2       # foot height
SCREW_X = 29.2     # screw hole x
SCREW_D = 8.0
SCREW_CH = 1.1     # chamfer at the top of the screw holes
CBORE_D = 10.6
CBORE_H = 3.0

xin = GAP / 2.0
half_w = W / 2.0 - xin


def rrect(w, l, r, z0, h, xc):
    return (cq.Workplane("XY").workplane(offset=z0).center(xc, 0)
            .rect(w, l).extrude(h).edges("|Z").fillet(r))


def _corner_edges(wp, xs, ys):
    out = []
    for e in wp.edges("|Z").vals():
        if e.geomType() != "LINE":
            continue
        p = e.Center()
        if any(abs(p.x - x) < 1e-6 for x in xs) and any(abs(p.y - y) < 1e-6 for y in ys):
            out.append(e)
    return out


def half_block(sign):
    """One half of the body (sign=+1 -> +X half)."""
    xc = sign * (xin + half_w / 2.0)
    x_in, x_out = sign * xin, sign * W / 2.0
    # lower shell: chamfered bottom edges, rounded vertical corners
    base = (cq.Workplane("XY").center(xc, 0).rect(half_w, L).extrude(Z_PART)
            .faces("<Z").edges().chamfer(C_BOT))
    base = base.newObject(_corner_edges(base, [x_in], [L / 2])).fillet(R_BACK_IN)
    base = base.newObject(_corner_edges(base, [x_in, x_out], [L / 2, -L / 2])).fillet(R_V)
    # upper shell: slightly inset, rounded top edges
    cover = (rrect(half_w - 2 * STEP, L - 2 * STEP, R_V - STEP, Z_PART, H - Z_PART, xc)
             .faces(">Z").edges().fillet(R_TOP))
    return base.union(cover)


body = half_block(1).union(half_block(-1))

# U-channel from the back edge, ending in an arc around the disk
y_meet = U_Y - math.sqrt(U_R ** 2 - CH_HALF ** 2)
y_back = L / 2.0 + 5.0
chan = (cq.Workplane("XY").workplane(offset=Z_FLOOR)
        .moveTo(-CH_HALF, y_back).lineTo(-CH_HALF, y_meet)
        .threePointArc((0, U_Y - U_R), (CH_HALF, y_meet))
        .lineTo(CH_HALF, y_back).close().extrude(H))
body = body.cut(chan)

# side ledges inside the channel (screw bosses along the walls)
y_ledge0 = U_Y - math.sqrt(U_R ** 2 - LEDGE_IN ** 2) - 2.0
hole_ys = [HOLE_Y1 - 2 * HOLE_P, HOLE_Y1 - HOLE_P, HOLE_Y1]
foot_yc = hole_ys[1]
y_end = HOLE_Y1
for s in (1, -1):
    lw = CH_HALF - LEDGE_IN + 0.5
    ledge = (cq.Workplane("XY").workplane(offset=Z_FLOOR - 0.01)
             .center(s * (LEDGE_IN + lw / 2.0), (y_ledge0 + y_end) / 2.0)
             .rect(lw, y_end - y_ledge0).extrude(LEDGE_Z - Z_FLOOR + 0.01))
    boss = (cq.Workplane("XY").workplane(offset=Z_FLOOR - 0.01)
            .center(s * SCREW_X, y_end).circle(LEDGE_END_R)
            .extrude(LEDGE_Z - Z_FLOOR + 0.01))
    body = body.union(ledge).union(boss)

# ---------------- turntable disk ----------------
disk = (cq.Workplane("XY").workplane(offset=DISK_Z0).center(0, DISK_Y)
        .circle(DISK_R).extrude(Z_RING - DISK_Z0)
        .faces(">Z").workplane().circle(DISK_R2).extrude(Z_PAD - Z_RING))
# cross pocket
arm_y = (cq.Workplane("XY").workplane(offset=Z_RING)
         .center(0, DISK_Y).rect(ARM_Y_W, 2 * ARM_Y_L).extrude(H)
         .edges("|Z").fillet(ARM_R))
arm_x = (cq.Workplane("XY").workplane(offset=Z_RING)
         .center(0, DISK_Y).rect(2 * DISK_R + 2, ARM_X_W).extrude(H))
disk = disk.cut(arm_y).cut(arm_x)
# holes
disk = disk.cut(cq.Workplane("XY").center(0, DISK_Y).circle(HOLE_C / 2)
                .extrude(H * 2, both=True))
pts = [(HOLE_S_R * math.cos(a), DISK_Y + HOLE_S_R * math.sin(a))
       for a in (0, math.pi / 2, math.pi, 3 * math.pi / 2)]
disk = disk.cut(cq.Workplane("XY").pushPoints(pts).circle(HOLE_S / 2)
                .extrude(H * 2, both=True))
disk = disk.cut(cq.Workplane("XY").workplane(offset=-1).pushPoints(pts)
                .circle(HOLE_S_CB / 2).extrude(1 + DISK_Z0 + 2.0))
# shallow recess on the underside
disk = disk.cut(cq.Workplane("XY").workplane(offset=-1).center(0, DISK_Y)
                .circle(DISK_REC_R).extrude(1 + DISK_Z0 + 0.4))

# clear the body under the disk so the disk is a clean insert
body = body.cut(cq.Workplane("XY").workplane(offset=-1).center(0, DISK_Y)
                .circle(DISK_R).extrude(Z_FLOOR + 1.01))
body = body.union(disk)

# ---------------- bottom obround feet with counterbored holes ----------------
foot_len = 2 * HOLE_P + FOOT_W
for s in (1, -1):
    foot = (cq.Workplane("XY").workplane(offset=-FOOT_H)
            .center(s * FOOT_X, foot_yc)
            .slot2D(foot_len, FOOT_W, angle=90).extrude(FOOT_H + 0.5))
    body = body.union(foot)
    hp = [(s * SCREW_X, y) for y in hole_ys]
    # through holes up to the ledge level, chamfered at the top
    for (hx, hy) in hp:
        cutter = (cq.Workplane("XY").workplane(offset=-FOOT_H - 1).center(hx, hy)
                  .circle(SCREW_D / 2).extrude(LEDGE_Z - SCREW_CH + FOOT_H + 1)
                  .faces(">Z").workplane().circle(SCREW_D / 2)
                  .workplane(offset=SCREW_CH + 0.5).circle(SCREW_D / 2 + SCREW_CH + 0.5)
                  .loft())
        body = body.cut(cutter)
    body = body.cut(cq.Workplane("XY").workplane(offset=-FOOT_H - 1)
                    .pushPoints(hp).circle(CBORE_D / 2).extrude(1 + CBORE_H))

result = body
